import math
import cadquery as cq

# Octagonal cup / adapter: an octagon prism (rounded underneath) with a blind bore
# opening to the front (-Y), a rectangular boss with a small through hole on the
# inside of the closed back wall, and a slot through the bottom of the wall at the front.

# ---------------- driving dimensions (mm) ----------------
AF = 100.0            # octagon across flats
DEPTH = 44.0          # overall length along the bore axis (Y)
BOTTOM_R = 44.0       # radius of the rounded bottom (tangent to the two lower diagonal flats)
BORE_D = 77.6         # blind bore diameter
BACK_WALL = 5.5       # thickness of the closed back wall
BOSS_W = 13.4         # rectangular boss on the inside of the back wall (X)
BOSS_H = 26.4         # rectangular boss (Z)
BOSS_T = 7.7          # boss height (towards the open front)
HOLE_D = 2.8          # small through hole at the centre of boss and back wall
SLOT_W = 18.0         # width of the bottom slot (X)
SLOT_DEPTH = 27.5     # length of the bottom slot from the front face (Y)
EDGE_R = 1.0          # small edge round on front / back rims and slot edges
BOSS_R = 1.0          # round on the front rim of the boss
HOLE_R = 0.5          # round on the ends of the centre hole

# ---------------- outer profile (XZ plane) ----------------
h = AF / 2.0
s = h * math.tan(math.radians(22.5))          # half side length of the octagon
apex = h * math.sqrt(2.0)                      # lower diagonals would meet at z = -apex
zc = -apex + BOTTOM_R * math.sqrt(2.0)         # centre of the bottom arc
tx = BOTTOM_R / math.sqrt(2.0)
tz = zc - BOTTOM_R / math.sqrt(2.0)            # tangent points of the bottom arc (+-tx, tz)

prof = (
    cq.Workplane("XZ")
    .moveTo(-s, h)
    .lineTo(s, h)
    .lineTo(h, s)
    .lineTo(h, -s)
    .lineTo(tx, tz)
    .threePointArc((0.0, zc - BOTTOM_R), (-tx, tz))
    .lineTo(-h, -s)
    .lineTo(-h, s)
    .close()
)
# the XZ workplane normal is -Y: extrude negative so the body runs from y=0 (front) to y=DEPTH (back)
body = prof.extrude(-DEPTH)

# ---------------- blind bore from the front face ----------------
bore_depth = DEPTH - BACK_WALL
bore = cq.Workplane("XZ").circle(BORE_D / 2.0).extrude(-bore_depth)
body = body.cut(bore)

# ---------------- slot through the bottom of the wall at the front ----------------
slot = (
    cq.Workplane("XY")
    .center(0, SLOT_DEPTH / 2.0 - 1.0)
    .rect(SLOT_W, SLOT_DEPTH + 2.0)
    .extrude(-(apex + 5.0))
)
body = body.cut(slot)

# ---------------- small edge rounds ----------------
# every edge except the long outer edges of the prism (kept sharp) and the bore-bottom circle
_tol = 1e-3


class _RoundEdges(cq.Selector):
    def filter(self, objs):
        out = []
        for e in objs:
            bb = e.BoundingBox()
            if bb.ylen > DEPTH - 0.1 and bb.xlen < 0.01 and bb.zlen < 0.01:
                continue  # long straight outer edges along Y
            if abs(bb.ymin - bore_depth) < _tol and abs(bb.ymax - bore_depth) < _tol:
                continue  # bore bottom circle
            out.append(e)
        return out


body = body.edges(_RoundEdges()).fillet(EDGE_R)

# ---------------- rectangular boss on the inner face of the back wall ----------------
boss = (
    cq.Workplane("XZ", origin=(0, bore_depth, 0))
    .rect(BOSS_W, BOSS_H)
    .extrude(BOSS_T)
)
body = body.union(boss)
boss_face_y = bore_depth - BOSS_T
body = body.edges(
    cq.selectors.BoxSelector(
        (-BOSS_W, boss_face_y - 0.01, -BOSS_H), (BOSS_W, boss_face_y + 0.01, BOSS_H)
    )
).fillet(BOSS_R)

# ---------------- small centre hole through boss and back wall ----------------
hole = (
    cq.Workplane("XZ", origin=(0, -1.0, 0))
    .circle(HOLE_D / 2.0)
    .extrude(-(DEPTH + 2.0))
)
body = body.cut(hole)
for _y in (boss_face_y, DEPTH):
    body = body.edges(
        cq.selectors.BoxSelector((-HOLE_D, _y - 0.01, -HOLE_D), (HOLE_D, _y + 0.01, HOLE_D))
    ).fillet(HOLE_R)

result = body

# ---------------- cosmetic seam on the rounded underside ----------------
# the reference shows the rounded bottom face split where the back wall starts
try:
    _shp = result.val()
    _edge = cq.Edge.makeThreePointArc(
        cq.Vector(tx, bore_depth, tz),
        cq.Vector(0.0, bore_depth, zc - BOTTOM_R),
        cq.Vector(-tx, bore_depth, tz),
    )
    _sol = _shp.split(_edge).Solids()
    if (
        len(_sol) == 1
        and _sol[0].isValid()
        and abs(_sol[0].Volume() - _shp.Volume()) < 1e-4 * _shp.Volume()
    ):
        result = cq.Workplane("XY").newObject([_sol[0]])
except Exception:
    result = body

VIEW = {"azimuth": 45, "elevation": 26}
